import cadquery as cq

# ---- driving dimensions (mm) ----
disc_d = 20.0       # flange diameter
disc_t = 8.25       # flange thickness
boss_d = 10.1       # rear boss diameter
boss_l = 3.2        # rear boss length
sq_w = 12.45        # square shank width (across flats)
sq_l = 16.7         # square shank length
sq_r = 1.7          # square shank corner radius (lengthwise edges)
pin_d = 8.3         # front pin diameter
pin_l = 12.4        # front pin length
pin_base_r = 2.0    # fillet pin -> square shank face
pin_tip_r = 2.0     # rounded pin tip

# The part is built along +Z (rear boss at the bottom, pin on top) and then
# turned so the pin points toward -Y (flange at the back, +Y side).
# Local x-direction of the sketch planes is -Y so the cylinder seams end up
# on the underside after the final rotation.


def wp(z):
    return cq.Workplane(cq.Plane(origin=(0, 0, z), xDir=(0, -1, 0), normal=(0, 0, 1)))


z_disc = 0.0
z_sq = z_disc + disc_t
z_pin = z_sq + sq_l

# rear boss
boss = wp(-boss_l).circle(boss_d / 2).extrude(boss_l)

# flange disc
disc = wp(z_disc).circle(disc_d / 2).extrude(disc_t)

# square shank with rounded lengthwise edges
shank = (wp(z_sq).rect(sq_w, sq_w).extrude(sq_l)
         .edges("|Z").fillet(sq_r))

# front pin with rounded tip
pin = (wp(z_pin).circle(pin_d / 2).extrude(pin_l)
       .faces(">Z").edges().fillet(pin_tip_r))

body = boss.union(disc).union(shank).union(pin)

# fillet where the pin meets the shank face
e = pin_d / 2 + 0.3
body = body.edges(cq.selectors.BoxSelector((-e, -e, z_pin - 0.05), (e, e, z_pin + 0.05),
                                          boundingbox=True)).fillet(pin_base_r)

# pin toward -Y, flange/boss toward +Y
result = body.rotate((0, 0, 0), (1, 0, 0), 90)

VIEW = {"azimuth": 45, "elevation": 26}
